import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # overall length along X
D = 58.0           # overall depth along Y
H_WALL = 10.4      # height of side / back walls
H_LIP = 11.4       # height of the thin front lip (taller than the walls)
T_WALL = 3.3       # side / back wall thickness
T_LIP = 3.3        # front lip thickness
CHAMFER = 2.6      # 45 deg chamfer around the bottom edge
FLOOR_Z = 3.75     # top of the pocket floor

BOSS_D = 15.5      # large boss diameter
BOSS_H = 4.5       # large boss height above floor
TOP_D = 8.6        # small upper boss diameter
TOP_H = 2.0        # small upper boss height
HOLE_D = 4.7       # blind hole diameter
HOLE_DEPTH = 6.0   # blind hole depth from top of small boss
SEAM_ANGLE = 45.0  # put cylinder seams on the silhouette

# boss centres (x, y)
BOSSES = [(-36.3, 13.5), (36.3, 13.5), (-18.2, -10.4), (18.2, -10.4)]

# engraved label on the underside
TEXT = "LM Module"
TEXT_SIZE = 10.5
TEXT_DEPTH = 0.4
TEXT_X = -13.2     # centre of the text (x)
TEXT_Y = -0.1      # centre of the text (y)
LOGO_GROOVE = 0.7  # width of the engraved logo outline

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .box(W, D, H_LIP, centered=(True, True, False))
    .edges("<Z")
    .chamfer(CHAMFER)
)

# lower the side / back walls: remove everything above H_WALL behind the lip
cut_top = (
    cq.Workplane("XY")
    .box(W + 2, D - T_LIP + 1, H_LIP, centered=(True, False, False))
    .translate((0, -D / 2 + T_LIP, H_WALL))
)
body = body.cut(cut_top)

# pocket
pocket = (
    cq.Workplane("XY")
    .box(W - 2 * T_WALL, D - T_WALL - T_LIP, H_LIP, centered=(True, False, False))
    .translate((0, -D / 2 + T_LIP, FLOOR_Z))
)
body = body.cut(pocket)

# stepped bosses with blind holes
for (x, y) in BOSSES:
    b = (
        cq.Workplane("XY")
        .workplane(offset=FLOOR_Z - 0.5)
        .circle(BOSS_D / 2)
        .extrude(BOSS_H + 0.5)
        .faces(">Z")
        .workplane()
        .circle(TOP_D / 2)
        .extrude(TOP_H)
    )
    hole = (
        cq.Workplane("XY")
        .workplane(offset=FLOOR_Z + BOSS_H + TOP_H - HOLE_DEPTH)
        .circle(HOLE_D / 2)
        .extrude(HOLE_DEPTH + 1)
    )
    b = b.cut(hole).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).translate((x, y, 0))
    body = body.union(b)
    body = body.cut(hole.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE).translate((x, y, 0)))

# engraved "LM Module" text on the underside (reads correctly from below)
try:
    label = cq.Workplane("XY").text(
        TEXT, TEXT_SIZE, TEXT_DEPTH, combine=False, halign="center", valign="center"
    )
    label = label.mirror("XZ").translate((TEXT_X, TEXT_Y, -0.01))
    body = body.cut(label)
except Exception:
    pass

# engraved logo (outline drawing) next to the text, made of straight strokes
LOGO_PTS = [
    (23.4, -4.4),   # left corner
    (19.5, 3.6),    # lower left
    (34.4, 3.9),    # lower kink
    (41.4, 9.9),    # tip
    (40.5, -4.5),   # upper right
    (37.7, -3.9),   # wavy upper edge ...
    (34.6, -4.4),
    (31.8, -5.0),
    (27.4, -4.9),
]
LOGO_DIVIDER = ((31.8, -5.1), (28.6, 3.6))


def stroke(p1, p2, w, depth):
    mx, my = (p1[0] + p2[0]) / 2, (p1[1] + p2[1]) / 2
    dx, dy = p2[0] - p1[0], p2[1] - p1[1]
    ln = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    return (
        cq.Workplane("XY")
        .center(mx, my)
        .slot2D(ln + w, w, ang)
        .extrude(depth)
    )


try:
    logo = None
    segs = [(LOGO_PTS[i], LOGO_PTS[(i + 1) % len(LOGO_PTS)]) for i in range(len(LOGO_PTS))]
    segs.append(LOGO_DIVIDER)
    for p1, p2 in segs:
        st = stroke(p1, p2, LOGO_GROOVE, TEXT_DEPTH + 0.01)
        logo = st if logo is None else logo.union(st)
    body = body.cut(logo.translate((0, 0, -0.01)))
except Exception:
    pass

result = body
